import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
pitch = 10.0          # centre-to-centre spacing of the square holes
n_cols = 16           # number of holes along X
n_rows = 16           # number of holes along Y
hole = 8.0            # square hole size (web between holes = pitch - hole)
strip = 10.0          # solid (unperforated) strip along the +X edge
thick = 2.0           # plate thickness

# ---------------- derived ----------------
grid_w = n_cols * pitch           # perforated zone width (X)
grid_d = n_rows * pitch           # perforated zone depth (Y)
W = grid_w + strip                # overall plate width (X)
D = grid_d                        # overall plate depth (Y)

# plate centred on the origin, bottom face on Z = 0
plate = cq.Workplane("XY").box(W, D, thick, centered=(True, True, False))

# hole grid centred on the perforated zone (which sits on the -X side)
grid_cx = -W / 2 + grid_w / 2
holes = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .center(grid_cx, 0)
    .rarray(pitch, pitch, n_cols, n_rows)
    .rect(hole, hole)
    .extrude(thick + 2.0)
)

result = plate.cut(holes)

VIEW = {"azimuth": 45, "elevation": 26}
